import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R_BODY = 30.0          # main body radius
R_BOT = 23.7           # radius of the flat bottom face
H_BOT_CH = 21.0        # height of the bottom conical chamfer
H_BODY = 83.55         # height of the straight cylindrical body
H_CONE = 54.45         # height of the shoulder cone
R_NECK = 13.5          # neck radius
H_NECK = 17.0          # neck height

GROOVE_W = 0.4         # decorative groove width
GROOVE_D = 0.2         # decorative groove depth
BODY_GROOVES = [78.8, 85.1]     # z of grooves on the body
CONE_GROOVES = [124.4, 134.3]   # z of grooves on the shoulder cone

SEAM_ANGLE = 180.0     # put the revolve seam at the back of the default view

VIEW = {"azimuth": 45, "elevation": 26}

z_body_bot = H_BOT_CH
z_body_top = H_BOT_CH + H_BODY
z_cone_top = z_body_top + H_CONE
H_TOTAL = z_cone_top + H_NECK


def revolve_profile(pts):
    """revolve a closed (r, z) profile drawn in the XZ plane about the Z axis"""
    return (cq.Workplane("XZ").polyline(pts).close()
            .revolve(360, (0, 0, 0), (0, 1, 0)))


# ---------------- main revolved body ----------------
profile = [
    (0, 0),
    (R_BOT, 0),
    (R_BODY, z_body_bot),
    (R_BODY, z_body_top),
    (R_NECK, z_cone_top),
    (R_NECK, H_TOTAL),
    (0, H_TOTAL),
]
body = revolve_profile(profile)


def cone_radius(z):
    t = (z - z_body_top) / H_CONE
    return R_BODY + (R_NECK - R_BODY) * t


def body_radius(z):
    return R_BODY


def groove_ring(z, radius_at):
    """thin V-shaped annular groove cutter at height z; lips sit on the surface"""
    z_lo, z_hi = z - GROOVE_W / 2, z + GROOVE_W / 2
    r_lo, r_hi, r_mid = radius_at(z_lo), radius_at(z_hi), radius_at(z)
    pts = [
        (r_lo + 2.0, z_lo - 0.5),
        (r_hi + 2.0, z_hi + 0.5),
        (r_hi + 2.0, z_hi),
        (r_hi, z_hi),
        (r_mid - GROOVE_D, z),
        (r_lo, z_lo),
        (r_lo + 2.0, z_lo),
    ]
    return revolve_profile(pts)


# ---------------- decorative grooves ----------------
for z in BODY_GROOVES:
    body = body.cut(groove_ring(z, body_radius))
for z in CONE_GROOVES:
    body = body.cut(groove_ring(z, cone_radius))

result = body.rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)
